import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 1.5          # gear module
N_TEETH = 14          # number of teeth
PRESSURE_ANGLE = 20.0 # degrees
FACE_WIDTH = 5.0      # gear face width (along X)
BORE_D = 5.0          # through bore
HUB_D = 14.0          # hub diameter
HUB_LEN = 5.0         # hub length (extends toward -X)
HUB_FLAT = 5.0        # distance of hub flat from axis (on -Y side)
SETSCREW_D = 2.6      # radial set-screw hole through the flat
BACKLASH = 0.25       # tooth thinning at the pitch circle
FLANK_PTS = 6         # spline points per involute flank
BORE_SEAM_DEG = 216.0 # angular position of the bore cylinder seam (cosmetic)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- gear geometry ----------------
rp = MODULE * N_TEETH / 2.0                 # pitch radius
ra = rp + MODULE                            # tip radius
rf = rp - 1.25 * MODULE                     # root radius
alpha = math.radians(PRESSURE_ANGLE)
rb = rp * math.cos(alpha)                   # base radius


def inv(a):
    return math.tan(a) - a


psi_b = math.pi / (2 * N_TEETH) + inv(alpha) - BACKLASH / (2 * rp)  # half tooth angle at base circle


def half_angle(r):
    if r <= rb:
        return psi_b
    return psi_b - inv(math.acos(rb / r))


def pol(r, t):
    # profile is drawn in the YZ plane: (u, v) -> (Y, Z); tooth 0 points to +Z
    return cq.Vector(0.0, r * math.cos(t), r * math.sin(t))


# below the base circle the flank runs parallel to the tooth centre line
hw_base = rb * math.sin(psi_b)
psi_root = math.asin(hw_base / rf)

pitch = 2 * math.pi / N_TEETH
r_start = max(rb, rf)
rs = [r_start + (ra - r_start) * (i / (FLANK_PTS - 1)) ** 1.5 for i in range(FLANK_PTS)]


def flank(c, side):
    """One smooth flank (root -> tip) for the tooth centred at angle c.
    side = -1 for the flank on the lower-angle side, +1 for the other."""
    pts = [pol(rf, c + side * psi_root)] + [pol(r, c + side * half_angle(r)) for r in rs[1:]]
    t0 = pol(1.0, c)                                   # start: parallel to the tooth centre line
    eps = 1e-3
    t1 = pol(ra, c + side * half_angle(ra)) - pol(ra - eps, c + side * half_angle(ra - eps))
    return pts, [t0, t1.normalized()]


edges = []
for k in range(N_TEETH):
    c = math.pi / 2 + k * pitch     # tooth centre angle
    rpts, rtan = flank(c, -1)
    lpts, ltan = flank(c, +1)
    # right flank root -> tip
    edges.append(cq.Edge.makeSpline(rpts, tangents=rtan))
    # tip arc
    edges.append(cq.Edge.makeThreePointArc(rpts[-1], pol(ra, c), lpts[-1]))
    # left flank tip -> root
    edges.append(cq.Edge.makeSpline(lpts[::-1], tangents=[-ltan[1], -ltan[0]]))
    # straight root land to the next tooth
    edges.append(cq.Edge.makeLine(lpts[0], pol(rf, c + pitch - psi_root)))

wire = cq.Wire.assembleEdges(edges)
face = cq.Face.makeFromWires(wire)
gear = cq.Workplane("YZ").add(cq.Solid.extrudeLinear(face, cq.Vector(FACE_WIDTH, 0, 0)))

# ---------------- hub with flat ----------------
hub = (
    cq.Workplane("YZ")
    .workplane(offset=-HUB_LEN)
    .circle(HUB_D / 2.0)
    .extrude(HUB_LEN)
)
flat_cut = (
    cq.Workplane("XY")
    .box(HUB_LEN * 4, HUB_D, HUB_D * 2)
    .translate((0, -HUB_FLAT - HUB_D / 2.0, 0))
)
hub = hub.cut(flat_cut)

body = gear.union(hub)

# ---------------- bore ----------------
bore = (
    cq.Workplane("YZ")
    .workplane(offset=-HUB_LEN - 1)
    .circle(BORE_D / 2.0)
    .extrude(HUB_LEN + FACE_WIDTH + 2)
    .rotate((0, 0, 0), (1, 0, 0), BORE_SEAM_DEG)   # place the cylinder seam
)
body = body.cut(bore)

# ---------------- radial set-screw hole through the flat ----------------
setscrew = (
    cq.Workplane("XZ")
    .workplane(offset=0)
    .center(-HUB_LEN / 2.0, 0)
    .circle(SETSCREW_D / 2.0)
    .extrude(HUB_D)      # XZ normal is -Y, so this extrudes toward -Y
)
body = body.cut(setscrew)

result = body
